import math
import cadquery as cq

# ---------------------------------------------------------------
# Bent sheet-metal tray with a V-shaped trough, long slot and tabs
# All driving dimensions below are in "design units"; S scales to mm
# ---------------------------------------------------------------
S = 0.5                      # mm per design unit

T = 7.2 * S                  # sheet thickness
THETA = math.radians(40.0)   # trough wall angle from horizontal
D = 24.5 * S                 # trough depth (top surface to top surface)
XL_IN = 14.0 * S             # half width of trough floor (top/inner surface)
XU_IN = XL_IN + D / math.tan(THETA)   # half width of trough at rim (top)
E = T * math.tan(THETA / 2)  # outer-corner offset of a sharp bend

X_LEFT = -107.3 * S          # left end of the part
X_RIGHT = 129.7 * S          # right end of the part
W_FLAT = 53.9 * S            # half width (Y) of the flat wings
W_BAND = 72.2 * S            # half width (Y) of the trough band
R_CORNER_L = 12.5 * S        # plan radius of the outer corners, left end
R_CORNER_R = 11.5 * S        # plan radius of the outer corners, right end

EAR_X0 = 51.2 * S            # where the 45 deg ear chamfer leaves the wing edge
W_STEP = 64.5 * S            # ear steps out to this half width at the rim bend
EAR_X1 = 35.6 * S            # wall chamfer meets the band edge (profile at z=T)
EAR_TILT = THETA / 2         # wing ear cut follows the rim-bend bisector

# edge notches (trapezoid, 45 deg sides)
NOTCH_L_X, NOTCH_L_W, NOTCH_L_D = -81.15 * S, 25.3 * S, 6.4 * S
NOTCH_R_X, NOTCH_R_W, NOTCH_R_D = 88.95 * S, 22.3 * S, 5.8 * S

# long slot through trough
SLOT_W2 = 15.4 * S           # half width of slot
SLOT_L_END = -42.9 * S       # left flat end
SLOT_L_CH = 9.2 * S          # left end chamfer
SLOT_R_END = 87.4 * S        # right flat end
SLOT_R_CH = 9.2 * S          # right end chamfer

# tabs
TAB_T = 7.1 * S              # tab thickness (X)
TAB_H = 20.4 * S             # tab height above wing top surface
TAB_Y0 = 16.0 * S            # inner Y face of outer tabs
TAB_Y1 = 33.4 * S            # outer Y face of tabs
TAB_LO_X = -75.6 * S         # left outer tab, min x
TAB_LI_X = -32.9 * S         # left inner tab (on trough wall), min x
WALL_RI_X = 78.6 * S         # right inner wall, min x
TAB_RO_X = 121.3 * S         # right outer tab, min x
LEDGE_DROP = 1.1 * S         # ledge of inner-left tab below wing top
LEDGE_FILLET = 1.4 * S       # fillet between ledge and tab
FOOT_X = 2.0 * S             # inset of the stepped foot below the tab
STEP_UP = 0.7 * S            # +X face of tab turns down here (above wing top)
TAB_HOLE_D = 2.0 * S
TAB_HOLE_Z = 10.2 * S        # above wing top

# holes along the lower bends
BEND_HOLE_D = 4.2 * S
BEND_HOLE_X = 15.9 * S       # |x| of the holes along the lower bends
BEND_HOLE_UP = 3.0 * S       # depth of hole centre below trough floor top

# ---------------------------------------------------------------
# sheet cross-section (XZ) extruded along Y
# ---------------------------------------------------------------
prof = [
    (X_LEFT, 0), (X_LEFT, T), (-XU_IN, T), (-XL_IN, T - D), (XL_IN, T - D),
    (XU_IN, T), (X_RIGHT, T), (X_RIGHT, 0), (XU_IN + E, 0), (XL_IN + E, -D),
    (-XL_IN - E, -D), (-XU_IN - E, 0),
]
sheet = (cq.Workplane("XZ").polyline(prof).close()
         .extrude(W_BAND, both=True))

ZB = -D - 10
ZH = 2 * (D + T + TAB_H + 10)


def prism(pts):
    """vertical prism through everything from a plan polygon"""
    return (cq.Workplane("XY").workplane(offset=ZB).polyline(pts).close()
            .extrude(ZH))


EAR_DIR = cq.Vector(math.sin(EAR_TILT), 0, math.cos(EAR_TILT))


def tilted_prism(pts, lean):
    """prism from a plan polygon drawn at the wing top (z=T), swept along a
    direction leaning 'lean' (+1 toward +X, -1 toward -X) as it rises"""
    d = cq.Vector(lean * EAR_DIR.x, 0, EAR_DIR.z)
    L = 3.0 * (D + T + 10)
    w = cq.Wire.makePolygon([cq.Vector(x, y, T) for x, y in pts], close=True)
    f = cq.Face.makeFromWires(w).translate(d * (-L / 2))
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(f, d * L))


cuts = []
for sy in (1, -1):
    # wings narrower than the trough band
    cuts.append(prism([(X_LEFT - 5, sy * W_FLAT), (-EAR_X0 - 5, sy * W_FLAT),
                       (-EAR_X0 - 5, sy * (W_BAND + 5)), (X_LEFT - 5, sy * (W_BAND + 5))]))
    cuts.append(prism([(EAR_X0 + 5, sy * W_FLAT), (X_RIGHT + 5, sy * W_FLAT),
                       (X_RIGHT + 5, sy * (W_BAND + 5)), (EAR_X0 + 5, sy * (W_BAND + 5))]))
    # ear chamfers: 45 deg on the wing (cut along the bend bisector), a small
    # step out at the rim bend, then a steeper chamfer down the trough wall
    yb = W_FLAT + (EAR_X0 - XU_IN)
    for sx in (1, -1):
        cuts.append(tilted_prism(
            [(sx * EAR_X0, sy * W_FLAT), (sx * XU_IN, sy * yb),
             (sx * XU_IN, sy * (W_BAND + 10)),
             (sx * (EAR_X0 + 12), sy * (W_BAND + 10)),
             (sx * (EAR_X0 + 12), sy * W_FLAT)], -sx))
        cuts.append(tilted_prism(
            [(sx * (XU_IN + 2 * E + 1), sy * W_STEP), (sx * XU_IN, sy * W_STEP),
             (sx * EAR_X1, sy * W_BAND), (sx * EAR_X1, sy * (W_BAND + 10)),
             (sx * (XU_IN + 2 * E + 1), sy * (W_BAND + 10))], -sx))
    # edge notches
    for nx, nw, nd in ((NOTCH_L_X, NOTCH_L_W, NOTCH_L_D),
                       (NOTCH_R_X, NOTCH_R_W, NOTCH_R_D)):
        cuts.append(prism([(nx - nw / 2, sy * (W_FLAT + 1)), (nx - nw / 2, sy * W_FLAT),
                           (nx - nw / 2 + nd, sy * (W_FLAT - nd)),
                           (nx + nw / 2 - nd, sy * (W_FLAT - nd)),
                           (nx + nw / 2, sy * W_FLAT), (nx + nw / 2, sy * (W_FLAT + 1))]))

# rounded outer corners
for cx, sx, R_CORNER in ((X_LEFT, -1, R_CORNER_L), (X_RIGHT, 1, R_CORNER_R)):
    for sy in (1, -1):
        ccx = cx - sx * R_CORNER
        ccy = sy * (W_FLAT - R_CORNER)
        blk = (cq.Workplane("XY").workplane(offset=ZB)
               .center(ccx + sx * R_CORNER / 2 + sx * 0.5, ccy + sy * R_CORNER / 2 + sy * 0.5)
               .rect(R_CORNER + 1, R_CORNER + 1).extrude(ZH))
        cyl = (cq.Workplane("XY").workplane(offset=ZB).center(ccx, ccy)
               .circle(R_CORNER).extrude(ZH))
        cuts.append(blk.cut(cyl))

for c in cuts:
    sheet = sheet.cut(c)

# ---------------------------------------------------------------
# tabs
# ---------------------------------------------------------------
z_top = T
tabs = []
for sy in (1, -1):
    y0, y1 = sy * TAB_Y0, sy * TAB_Y1
    ylo, yhi = min(y0, y1), max(y0, y1)
    for x0 in (TAB_LO_X, TAB_RO_X):
        tabs.append(cq.Workplane("XY").box(TAB_T, yhi - ylo, TAB_H, centered=False)
                    .translate((x0, ylo, z_top)))

# right inner wall (slot is cut through it later)
tabs.append(cq.Workplane("XY").box(TAB_T, 2 * TAB_Y1, TAB_H, centered=False)
            .translate((WALL_RI_X, -TAB_Y1, z_top)))

# left inner tabs standing on the trough wall, with a ledge at the base
tanT = math.tan(THETA)


def wall_top_z(x):
    return T - (x + XU_IN) * tanT


xa = TAB_LI_X
xb = TAB_LI_X + TAB_T
x_ledge = -XU_IN + LEDGE_DROP / tanT     # ledge meets the wall surface here
x_foot = xa + FOOT_X                     # foot of the stiffening step
z_step = T + STEP_UP                     # where the +X face turns down
z_foot = z_step - (xb - x_foot) * tanT   # step runs parallel to the wall
zl = T - LEDGE_DROP
rf = LEDGE_FILLET
li_wall = (cq.Workplane("XZ")
           .moveTo(x_ledge, zl).lineTo(xa - rf, zl)
           .radiusArc((xa, zl + rf), -rf)
           .lineTo(xa, T + TAB_H).lineTo(xb, T + TAB_H).lineTo(xb, z_step)
           .lineTo(x_foot, z_foot).lineTo(x_foot, wall_top_z(x_foot) - 3.0 * S)
           .lineTo(x_ledge, wall_top_z(x_ledge) - 3.0 * S).close()
           .extrude(TAB_Y1, both=True))
tabs.append(li_wall)

part = sheet
for t in tabs:
    part = part.union(t)

# ---------------------------------------------------------------
# slot through trough, chamfered ends
# ---------------------------------------------------------------
slot_pts = [
    (SLOT_L_END, -SLOT_W2 + SLOT_L_CH), (SLOT_L_END + SLOT_L_CH, -SLOT_W2),
    (SLOT_R_END - SLOT_R_CH, -SLOT_W2), (SLOT_R_END, -SLOT_W2 + SLOT_R_CH),
    (SLOT_R_END, SLOT_W2 - SLOT_R_CH), (SLOT_R_END - SLOT_R_CH, SLOT_W2),
    (SLOT_L_END + SLOT_L_CH, SLOT_W2), (SLOT_L_END, SLOT_W2 - SLOT_L_CH),
]
part = part.cut(prism(slot_pts))

# ---------------------------------------------------------------
# holes: pin holes through tabs (along Y), holes along lower bends
# ---------------------------------------------------------------
hz = T + TAB_HOLE_Z
for xc in (TAB_LO_X + TAB_T / 2, TAB_LI_X + TAB_T / 2, WALL_RI_X + TAB_T / 2,
           TAB_RO_X + TAB_T / 2):
    h = (cq.Workplane("XZ", origin=(0, TAB_Y1 + 1, 0)).center(xc, hz)
         .circle(TAB_HOLE_D / 2).extrude(2 * TAB_Y1 + 2))
    part = part.cut(h)

bz = T - D - BEND_HOLE_UP
for sx in (1, -1):
    xc = sx * BEND_HOLE_X
    h = (cq.Workplane("XZ", origin=(0, W_BAND + 1, 0)).center(xc, bz)
         .circle(BEND_HOLE_D / 2).extrude(2 * W_BAND + 2))
    part = part.cut(h)

result = part
VIEW = {"azimuth": 45, "elevation": 26}
